import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Curved capstan-style sector arm (arc plate with lightening windows)
# Arc centre is at the origin, plate lies in XY, thickness along +Z.
# ---------------------------------------------------------------------------

R_OUT = 154.5        # outer rim radius
X_IN = 102.3         # straight inner edge (x = const)
T = 10.5             # plate thickness
TH_TOP = 53.0        # angle of the radial end face at the +Y end (deg)
TH_BOT = -45.0       # angle of the round lug at the -Y end (deg)

# lightening windows
WIN_X = 115.2        # inner boundary of windows (x = const)
WIN_R = 140.8        # outer boundary of windows (radius)
RIB_W = 8.5          # rib width
RIB_ANGLES = [-24.5, -12.25, 0.0, 12.25, 24.5]
WIN_FILLET = 1.5

# round lug at the -Y end
LUG_RC = 139.5       # radius of lug centre from arc centre
LUG_R = R_OUT - LUG_RC
SQ = 10.4            # square pocket side (both lugs)
LUG_SQ_D = 7.0       # square pocket depth
LUG_PIN_HOLE = 1.8
LUG_PIN_OFF = 8.2
LUG_PIN_DEPTH = 5.0
LUG_SIDE_HOLE = 2.7
LUG_SIDE_PHI = 223.0
LUG_SLOT_PHI = 160.0
LUG_SLOT_W = 2.8
LUG_SLOT_H = 5.6
LUG_SLOT_DEPTH = 6.0
LUG_SQ_OFF = 0.6      # pocket offset from lug centre towards the lug tip
LUG_NECK_FILLET = 4.0

# rectangular lug at the +Y end (frame rotated 45 deg: u=(1,1)/r2, v=(-1,1)/r2)
BLK_U0 = 126.2
BLK_U1 = 141.1
BLK_V0 = -10.8
BLK_V1 = 14.9
STEP_V = -4.0        # step edge of the lowered end strip
STRIP_H = T / 2.0    # remaining height of the lowered strip
NOTCH_U0 = 134.4
NOTCH_V0 = -4.0
NOTCH_FLOOR = 2.0
BLK_CORNER_R = 4.0
SMALL_HOLE = 2.0
STRIP_HOLES_UV = [(149.7, 17.1), (146.8, 9.7), (148.7, 1.3)]
STRIP_HOLE_D = 2.6
STRIP_CB_D = 4.5
STRIP_CB_DEPTH = 2.5
BLK_HOLE_UV = (131.5, 1.2)
BLK_HOLE_D = 2.5
BLIND_DEPTH = 5.0

# pin on the straight edge
PIN_D = 10.4
PIN_ROOT_L = 2.1     # length of the flared root
PIN_ROOT_R = 6.1     # radius of the flare where it meets the plate
PIN_L = 8.4
PIN_CHAMFER = 0.5
PIN_HOLE = 1.5

# rail holes near the +Y end
RAIL_HOLE_D = 5.0
RAIL_HOLE_X = 106.6
RAIL_HOLE_Y = [83.7, 72.5, 61.3]

# rim groove (cable track) + top chamfer, wraps onto the round lug
GROOVE_DEPTH = 1.0
GROOVE_Z0 = 1.6
GROOVE_Z1 = 8.5
GROOVE_CH = 0.6
TOP_CHAMFER = 1.0
GROOVE_END_PHI = -70.0   # end of the groove on the round lug (deg, around lug centre)
GROOVE_END_DEPTH = 2.0   # groove runs deeper into the lug towards its end

S2 = math.sqrt(0.5)


def uv(u, v):
    return ((u - v) * S2, (u + v) * S2)


def pol(r, a):
    return (r * math.cos(math.radians(a)), r * math.sin(math.radians(a)))


def prism(pts, z0=0.0, h=T):
    return cq.Workplane("XY").workplane(offset=z0).polyline(pts).close().extrude(h)


def cyl(x, y, d, z0=-1.0, h=T + 2):
    return cq.Workplane("XY").workplane(offset=z0).center(x, y).circle(d / 2).extrude(h)


def groove_profile(rs, d):
    c = GROOVE_CH
    return [(rs - d, GROOVE_Z0 + c), (rs, GROOVE_Z0), (rs + 3, GROOVE_Z0),
            (rs + 3, GROOVE_Z1), (rs, GROOVE_Z1), (rs - d, GROOVE_Z1 - c)]


def profile_wire(prof, ang, centre):
    ca, sa = math.cos(math.radians(ang)), math.sin(math.radians(ang))
    pts = [cq.Vector(centre[0] + r * ca, centre[1] + r * sa, z) for (r, z) in prof]
    return cq.Wire.makePolygon(pts, close=True)


def rim_cutter(rs, a0, a1, centre, end_depth=None):
    """groove + top chamfer profile revolved around a vertical axis.
    With end_depth the groove deepens linearly towards a0 (ruled loft)."""
    ch = TOP_CHAMFER
    cham = [(rs - ch - 1, T + 1), (rs, T - ch), (rs + 3, T - ch), (rs + 3, T + 1)]
    profs = [cham]
    if end_depth is None:
        profs.append(groove_profile(rs, GROOVE_DEPTH))
    out = None
    for prof in profs:
        s = (cq.Workplane("XZ").polyline(prof).close()
             .revolve(a1 - a0, (0, 0, 0), (0, 1, 0)))
        out = s if out is None else out.union(s)
    out = out.rotate((0, 0, 0), (0, 0, 1), a0).translate((centre[0], centre[1], 0))
    if end_depth is not None:
        w1 = profile_wire(groove_profile(rs, GROOVE_DEPTH), a1, centre)
        w0 = profile_wire(groove_profile(rs, end_depth), a0, centre)
        out = out.union(cq.Workplane("XY").add(cq.Solid.makeLoft([w1, w0], True)))
    return out


# ---------------------------------------------------------------- main body
disk = cq.Workplane("XY").circle(R_OUT).extrude(T)
wedge_pts = [(0, 0)] + [pol(400, TH_BOT + (TH_TOP - TH_BOT) * i / 8.0) for i in range(9)]
wedge = prism(wedge_pts, -1, T + 2)
hp_x = cq.Workplane("XY").center(X_IN + 200, 0).rect(400, 800).extrude(T)
hp_u = prism([uv(BLK_U1, -60), uv(400, -60), uv(400, 60), uv(BLK_U1, 60)])
body = disk.intersect(wedge).intersect(hp_x.union(hp_u))

# round lug
lug_c = pol(LUG_RC, TH_BOT)
lug = cq.Workplane("XY").center(*lug_c).circle(LUG_R).extrude(T)
body = body.union(lug)

# rectangular block at +Y end and filler step to the straight edge
blk = prism([uv(BLK_U0, BLK_V0), uv(BLK_U1, BLK_V0), uv(BLK_U1, BLK_V1), uv(BLK_U0, BLK_V1)])
c_low = uv(BLK_U0, BLK_V0)
fill = prism([c_low, (X_IN + 1.0, c_low[1]), (X_IN + 1.0, c_low[1] + (X_IN + 1.0 - c_low[0]))])
body = body.union(blk).union(fill)

# concave fillet between round lug and straight edge
neck_y = lug_c[1] + math.sqrt(LUG_R ** 2 - (X_IN - lug_c[0]) ** 2)
body = body.edges(cq.selectors.NearestToPointSelector((X_IN, neck_y, T / 2))).fillet(LUG_NECK_FILLET)
# rounded outer corner of the block
bc = uv(BLK_U0, BLK_V1)
body = body.edges(cq.selectors.NearestToPointSelector((bc[0], bc[1], T / 2))).fillet(BLK_CORNER_R)

# ---------------------------------------------------------------- rim groove + chamfer
body = body.cut(rim_cutter(R_OUT, TH_BOT, TH_TOP + 5, (0, 0)))
body = body.cut(rim_cutter(LUG_R, GROOVE_END_PHI, TH_BOT, lug_c, GROOVE_END_DEPTH))

# ---------------------------------------------------------------- pin
# revolved pin with a conical flared root, clipped to the plate thickness
pr = PIN_D / 2
pin = (cq.Workplane("XY")
       .moveTo(X_IN - PIN_L, 0)
       .lineTo(X_IN - PIN_L, pr - PIN_CHAMFER)
       .lineTo(X_IN - PIN_L + PIN_CHAMFER, pr)
       .lineTo(X_IN - PIN_ROOT_L, pr)
       .lineTo(X_IN, PIN_ROOT_R)
       .lineTo(X_IN + 1.0, PIN_ROOT_R)
       .lineTo(X_IN + 1.0, 0)
       .close()
       .revolve(360, (0, 0, 0), (1, 0, 0))
       .translate((0, 0, T / 2)))
pin = pin.intersect(cq.Workplane("XY").center(X_IN, 0).rect(40, 40).extrude(T))
body = body.union(pin)
pin_hole = (cq.Workplane("YZ").workplane(offset=X_IN - PIN_L - 1).center(0, T / 2)
            .circle(PIN_HOLE / 2).extrude(3.0))
body = body.cut(pin_hole)

# ---------------------------------------------------------------- windows
win = (cyl(0, 0, 2 * WIN_R)
       .intersect(cq.Workplane("XY").center(WIN_X + 100, 0).rect(200, 400).extrude(T + 2)
                  .translate((0, 0, -1))))
for a in RIB_ANGLES:
    rib = (cq.Workplane("XY").center(100, 0).rect(200, RIB_W).extrude(T + 4)
           .translate((0, 0, -2)).rotate((0, 0, 0), (0, 0, 1), a))
    win = win.cut(rib)
win = win.edges("|Z").fillet(WIN_FILLET)
body = body.cut(win)

# ---------------------------------------------------------------- small holes
for y in RAIL_HOLE_Y:
    body = body.cut(cyl(RAIL_HOLE_X, y, RAIL_HOLE_D))
for x in (WIN_X + 0.8, WIN_R - 0.8):
    body = body.cut(cyl(x, 0, SMALL_HOLE, T - BLIND_DEPTH, BLIND_DEPTH + 1))
for (u, v) in STRIP_HOLES_UV:
    p = uv(u, v)
    body = body.cut(cyl(p[0], p[1], STRIP_HOLE_D))
    body = body.cut(cyl(p[0], p[1], STRIP_CB_D, -1.0, STRIP_CB_DEPTH + 1.0))
p = uv(*BLK_HOLE_UV)
body = body.cut(cyl(p[0], p[1], BLK_HOLE_D, T - BLIND_DEPTH, BLIND_DEPTH + 1))
sq_c = (lug_c[0] - LUG_SQ_OFF * S2, lug_c[1] - LUG_SQ_OFF * S2)
for s in (-1, 1):
    hc = (sq_c[0] - s * LUG_PIN_OFF * S2, sq_c[1] + s * LUG_PIN_OFF * S2)
    body = body.cut(cyl(hc[0], hc[1], LUG_PIN_HOLE, T - LUG_PIN_DEPTH, LUG_PIN_DEPTH + 1))

# ---------------------------------------------------------------- round lug pocket, side hole, slot
sq = (cq.Workplane("XY").workplane(offset=T - LUG_SQ_D).center(*sq_c)
      .rect(SQ, SQ).extrude(LUG_SQ_D + 1)
      .rotate((sq_c[0], sq_c[1], 0), (sq_c[0], sq_c[1], 1), 45))
body = body.cut(sq)
side = (cq.Workplane("YZ").circle(LUG_SIDE_HOLE / 2).extrude(LUG_R + 2)
        .translate((0, 0, T / 2))
        .rotate((0, 0, 0), (0, 0, 1), LUG_SIDE_PHI)
        .translate((lug_c[0], lug_c[1], 0)))
body = body.cut(side)
slot = (cq.Workplane("XY").box(LUG_SLOT_DEPTH + 2, LUG_SLOT_W, LUG_SLOT_H, centered=(False, True, True))
        .translate((LUG_R - LUG_SLOT_DEPTH, 0, T / 2))
        .rotate((0, 0, 0), (0, 0, 1), LUG_SLOT_PHI)
        .translate((lug_c[0], lug_c[1], 0)))
body = body.cut(slot)

# ---------------------------------------------------------------- lowered end strip and square notch
strip = prism([uv(BLK_U1, STEP_V), uv(200, STEP_V), uv(200, 80), uv(BLK_U1, 80)],
              STRIP_H, T)
body = body.cut(strip)
notch = prism([uv(NOTCH_U0, NOTCH_V0), uv(NOTCH_U0 + SQ, NOTCH_V0),
               uv(NOTCH_U0 + SQ, NOTCH_V0 + SQ), uv(NOTCH_U0, NOTCH_V0 + SQ)],
              NOTCH_FLOOR, T)
body = body.cut(notch)

# ---------------------------------------------------------------- orientation
# the reference part sits rolled by about one degree about the Y axis
# (outer rim slightly higher than the inner edge)
TILT_Y = -1.0
result = body.rotate((117.0, 0, T / 2), (117.0, 1, T / 2), TILT_Y)
